import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
A_LONG = 79.4      # centre -> long edges (the three edges carrying arms)
A_SHORT = 88.8     # centre -> short edges (truncated corners)
T = 16.0           # plate thickness (arms are full height)
R_VERTEX = 4.0     # rounding of plate corners (plan view)

ARM_W = 7.5        # arm (fin) thickness
ARM_L = 29.5       # arm projection beyond the long edge
ARM_E = 47.5       # arm centre offset from long-edge midpoint
ARM_TIP_R = 7.0    # rounding of the top outer corner of arm tip (side view)
ARM_PLAN_R = 2.0   # rounding of arm tip corners (plan view)
ARM_ROOT_R = 4.0   # concave rounding, arm side facing the edge middle
ARM_ROOT_R2 = 2.5  # concave rounding, arm side facing the plate corner
HEX_AF = 6.0       # hexagonal through hole in each arm (across flats)
HEX_FROM_TIP = 9.5

SLOT_W = 33.6      # key slot outer width
SLOT_Y0 = -56.4    # front end of slot
SLOT_Y1 = 16.0     # back end of slot
LIP_T = 3.5        # lip (ledge) width inside the slot
LIP_Y0 = -27.5     # front end of lip (at the slot wall)
LIP_DEPTH = 5.0    # lip top below plate top

EAR_W = 20.5
EAR_X = 27.7       # ear centre offset from the slot axis
EAR_Y = 0.0        # front face of ears
EAR_H = 15.5       # height above plate top
EAR_TOP = 10.4     # flat top depth
EAR_SLOPE_L = 15.0 # horizontal run of the sloped back face
EAR_R = 1.8        # rounding of ear top edges (front view corners)
EAR_TOP_R = 2.5    # rounding between ear top and sloped back
EAR_BASE_R = 1.0   # fillet where the ears meet the plate
EAR_HOLE_D = 8.0
EAR_HOLE_Z = 7.75  # above plate top
EAR_CB_D = 14.8    # counterbore from the sloped back face
EAR_CB_Y = 5.0     # counterbore floor position

VIEW = {"azimuth": 45, "elevation": 26}

LONG_NORMALS = [270.0, 30.0, 150.0]


def frame(phi_deg):
    p = math.radians(phi_deg)
    n = (math.cos(p), math.sin(p))
    t = (-math.sin(p), math.cos(p))
    return n, t


def pt(n, t, a, s):
    return (a * n[0] + s * t[0], a * n[1] + s * t[1])


# ---------------- plate outline with arms (plan view) ----------------
def filleted_outline(corners):
    """corners: list of ((x, y), r) of a closed polygon; returns a closed
    Workplane wire with every corner rounded by its radius (convex or concave)"""
    n = len(corners)
    segs = []
    for i in range(n):
        p = corners[i][0]
        r = corners[i][1]
        a = corners[i - 1][0]
        b = corners[(i + 1) % n][0]
        d1 = (a[0] - p[0], a[1] - p[1])
        d2 = (b[0] - p[0], b[1] - p[1])
        l1 = math.hypot(*d1)
        l2 = math.hypot(*d2)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosang = max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))
        half = math.acos(cosang) / 2.0
        td = r / math.tan(half)
        t1 = (p[0] + d1[0] * td, p[1] + d1[1] * td)
        t2 = (p[0] + d2[0] * td, p[1] + d2[1] * td)
        bx, by = d1[0] + d2[0], d1[1] + d2[1]
        bl = math.hypot(bx, by)
        bx, by = bx / bl, by / bl
        cd = r / math.sin(half)
        c = (p[0] + bx * cd, p[1] + by * cd)
        m = (c[0] - bx * r, c[1] - by * r)
        segs.append((t1, m, t2))
    wp = cq.Workplane("XY").moveTo(*segs[0][0])
    for i in range(n):
        t1, m, t2 = segs[i]
        if i > 0:
            wp = wp.lineTo(*t1)
        wp = wp.threePointArc(m, t2)
    return wp.close()


half_long = (A_SHORT - 0.5 * A_LONG) / math.cos(math.radians(30))
corners = []
arm_frames = []
for phi in LONG_NORMALS:
    n, t = frame(phi)
    corners.append((pt(n, t, A_LONG, -half_long), R_VERTEX))
    for s in (-ARM_E, ARM_E):
        s0 = s - ARM_W / 2.0
        s1 = s + ARM_W / 2.0
        r0 = ARM_ROOT_R2 if s < 0 else ARM_ROOT_R
        r1 = ARM_ROOT_R if s < 0 else ARM_ROOT_R2
        corners.append((pt(n, t, A_LONG, s0), r0))
        corners.append((pt(n, t, A_LONG + ARM_L, s0), ARM_PLAN_R))
        corners.append((pt(n, t, A_LONG + ARM_L, s1), ARM_PLAN_R))
        corners.append((pt(n, t, A_LONG, s1), r1))
        arm_frames.append((n, t, pt(n, t, A_LONG, s)))
    corners.append((pt(n, t, A_LONG, half_long), R_VERTEX))

body = filleted_outline(corners).extrude(T)

# arm tips: round the top outer corner (side view) and add the hex hole
for (n, t, base) in arm_frames:
    ang = math.degrees(math.atan2(n[1], n[0]))
    u1 = ARM_L
    tool = (
        cq.Workplane("XZ")
        .moveTo(u1 - ARM_TIP_R, T + 1)
        .lineTo(u1 - ARM_TIP_R, T)
        .threePointArc(
            (u1 - ARM_TIP_R + ARM_TIP_R * math.cos(math.pi / 4),
             T - ARM_TIP_R + ARM_TIP_R * math.sin(math.pi / 4)),
            (u1, T - ARM_TIP_R),
        )
        .lineTo(u1 + 1, T - ARM_TIP_R)
        .lineTo(u1 + 1, T + 1)
        .close()
        .extrude(ARM_W, both=True)
    )
    hole = (
        cq.Workplane("XZ")
        .center(u1 - HEX_FROM_TIP, T / 2.0)
        .polygon(6, HEX_AF / math.cos(math.radians(30)))
        .extrude(ARM_W, both=True)
    )
    tool = tool.union(hole)
    tool = tool.rotate((0, 0, 0), (0, 0, 1), ang).translate((base[0], base[1], 0))
    body = body.cut(tool)

# ---------------- ears (pivot brackets) ----------------
def make_ear(xc):
    # side profile (Y-Z): vertical front, flat top, sloped back
    side = (
        cq.Workplane("YZ", origin=(xc - EAR_W / 2.0, 0, 0))
        .moveTo(EAR_Y, T - 0.5)
        .lineTo(EAR_Y, T + EAR_H)
        .lineTo(EAR_Y + EAR_TOP, T + EAR_H)
        .lineTo(EAR_Y + EAR_TOP + EAR_SLOPE_L * (EAR_H + 0.5) / EAR_H, T - 0.5)
        .close()
        .extrude(EAR_W)
    )
    side = side.edges(
        cq.selectors.NearestToPointSelector((xc, EAR_Y + EAR_TOP, T + EAR_H))
    ).fillet(EAR_TOP_R)
    # front profile (X-Z): rectangle with rounded top corners
    front = (
        cq.Workplane("XZ", origin=(0, EAR_Y - 1.0, 0))
        .center(xc, T - 0.5 + (EAR_H + 0.5) / 2.0)
        .rect(EAR_W, EAR_H + 0.5)
        .extrude(-(EAR_TOP + EAR_SLOPE_L + 4))
        .edges("|Y and >Z")
        .fillet(EAR_R)
    )
    ear = side.intersect(front)
    hole = (
        cq.Workplane("XZ", origin=(xc, EAR_Y - 1, T + EAR_HOLE_Z))
        .circle(EAR_HOLE_D / 2.0)
        .extrude(-(EAR_TOP + EAR_H + 4))
    )
    cb = (
        cq.Workplane("XZ", origin=(xc, EAR_Y + EAR_CB_Y, T + EAR_HOLE_Z))
        .circle(EAR_CB_D / 2.0)
        .extrude(-(EAR_TOP + EAR_H + 4))
    )
    return ear.cut(hole).cut(cb)


for xc in (-EAR_X, EAR_X):
    body = body.union(make_ear(xc))


class EarBase(cq.Selector):
    """edges where the ears sit on the plate top"""

    def filter(self, objs):
        out = []
        for o in objs:
            bb = o.BoundingBox()
            c = o.Center()
            if (abs(bb.zmin - T) < 1e-3 and abs(bb.zmax - T) < 1e-3
                    and -0.5 < c.y < EAR_TOP + EAR_SLOPE_L + 1
                    and abs(abs(c.x) - EAR_X) < EAR_W / 2.0 + 0.5):
                out.append(o)
        return out


body = body.edges(EarBase()).fillet(EAR_BASE_R)

# ---------------- key slot with internal lip ----------------
def stadium(w, y0, y1, z0, z1):
    return (
        cq.Workplane("XY", origin=(0, (y0 + y1) / 2.0, z0))
        .slot2D(y1 - y0, w, angle=90)
        .extrude(z1 - z0)
    )

lip_w = SLOT_W - 2 * LIP_T
upper = stadium(SLOT_W, SLOT_Y0, SLOT_Y1, T - LIP_DEPTH, T + 1)
inner = stadium(lip_w, SLOT_Y0 + LIP_T, SLOT_Y1 - LIP_T, -1, T + 1)
# front region is open full width; the lip ends are cut at 45 deg in plan
hw = SLOT_W / 2.0 + 1.0
front_cut = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .polyline([
        (-hw, SLOT_Y0 - 5),
        (hw, SLOT_Y0 - 5),
        (hw, LIP_Y0 - 1.0),
        (SLOT_W / 2.0, LIP_Y0),
        (lip_w / 2.0, LIP_Y0 + LIP_T),
        (-lip_w / 2.0, LIP_Y0 + LIP_T),
        (-SLOT_W / 2.0, LIP_Y0),
        (-hw, LIP_Y0 - 1.0),
    ]).close()
    .extrude(T + 2)
)
front = stadium(SLOT_W, SLOT_Y0, SLOT_Y1, -1, T + 1).intersect(front_cut)
body = body.cut(upper).cut(front).cut(inner)

result = body


